import cadquery as cq
import math

# =====================================================================
#  Row of three two-piece clips.  Each clip = two mirrored halves; each
#  half is a thin-walled shoe: a tall outer wall that tapers to a
#  chevron tip blade (-Y end) and flares inward at the +Y end, a low
#  inner bar + two low cross ribs, a box under a top plate carrying a
#  cylindrical peg, and a few bracing gussets.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
N_UNITS = 3          # clips side by side along X
PITCH = 40.0         # unit pitch along X
L = 101.0            # length along Y (tip at Y=0, flared end at Y=L)
H = 23.5             # wall height
WO = 19.1            # unit centre -> outer face of outer wall
T = 2.0              # wall thickness
TAPER_Y = 63.5       # outer wall is flat for Y > TAPER_Y and tapers toward the tip
BLADE_X = (7.2, 9.3) # tip blade (unit relative x range)
FLARE_OUT_X = 15.0   # outer face of the flared end at Y=L
TIP_CHEV = 10.7      # chevron depth at the tip end (side view)
END_CHEV = 6.5       # chevron depth at the flared end (side view)
ZC = 10.8            # height of the chevron point at the tip end
ZC_END = 11.9        # height of the chevron point at the flared end

# plan-view control points of the tapered part of the outer wall
TAPER_OUT = [(9.3, 0.0), (9.5, 12.0), (11.3, 20.0), (13.6, 30.0), (WO, TAPER_Y)]
TAPER_IN = [(7.2, 0.0), (7.4, 12.0), (9.2, 20.0), (11.5, 30.0), (WO - T, TAPER_Y)]
# plan-view control points of the flared outer face
FLARE_OUT = [(WO, TAPER_Y), (WO, 75.0), (WO - 0.1, 84.0), (18.4, 91.0),
             (16.4, 96.5), (FLARE_OUT_X, L)]
FLARE_IN_X = 12.5    # inner face of the flared end at Y=L
# plan-view control points of the flared inner face (from the end back to the wall)
FLARE_IN = [(FLARE_IN_X, L), (13.0, 97.0), (14.6, 93.0), (16.5, 89.5), (WO - T, 84.0)]

BAR_H = 4.2          # height of the low inner bar / ribs
BAR_W = 2.0          # inner bar width
BAR_IN_X = 0.7       # inner bar inner face at the lower rib
BAR_TIP_X = 6.2      # inner bar inner face where it meets the blade
BAR_Y0 = 11.0        # inner bar meets the blade here
GUS_RISE = 7.0       # V gusset top rises this much from the bar to the wall
GUSSET_Y = 25.0      # tip gusset between wall and inner bar ends here

RIB1_Y = (59.0, 63.0)    # lower rib (in front of the plate)
RIB2_Y = (83.6, 87.7)    # upper rib (near flared end)
RIB_HOLE_D = 1.2
RIB_CH = 1.2             # chamfer on the inner end of the ribs

PLATE_Y = (63.0, 76.4)   # peg plate extent in Y
PLATE_T = 2.0            # plate thickness above the wall top
PLATE_END_X = 0.55       # rounded end of the plate (unit relative)
PLATE_R = 5.8            # corner radius of the rounded end
PLATE_FLAT_X = 12.8      # where the plate bevel starts (toward the outer wall)
BEV_R = 3.0              # rounding of the plate bevel
PEG_X = 6.4
PEG_Y = 69.5
PEG_D = 6.0
PEG_H = 4.5

BOX_X0 = 11.3            # inner face of the box under the plate
BOX_WALL = 2.0
WIN = (2.0, 2.5, 21.3)   # notch at the front-inner-top corner of the box (right half
                         # only): width in x, depth in y, bottom z
GUSF_WALL_Y = 58.8       # diagonal front face of the front gusset meets the wall here
GUSF_X = 12.2            # ... and meets the box front here (also the gusset foot)
GUSF_Y0 = 57.0           # (approximate) front end of the front gusset
GUS2_Y1 = 93.2           # rear gusset runs along the wall up into the flare
GUS_X = 13.0             # foot of the sloped gussets (unit-relative x)


def poly_prism(pts, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0)
            .polyline(pts).close().extrude(z1 - z0))


def yz_prism(pts, x0, x1):
    """prism from a (Y, Z) profile extruded along X from x0 to x1"""
    return (cq.Workplane("YZ").workplane(offset=x0)
            .polyline(pts).close().extrude(x1 - x0))


def xz_prism(pts, y0, y1):
    """prism from an (X, Z) profile extruded along Y from y0 to y1"""
    return (cq.Workplane("XZ").workplane(offset=-y0)
            .polyline(pts).close().extrude(-(y1 - y0)))


def interp(pts, y):
    """linear interpolation of x along a list of (x, y) points"""
    for (xa, ya), (xb, yb) in zip(pts[:-1], pts[1:]):
        if ya <= y <= yb:
            return xa + (xb - xa) * (y - ya) / (yb - ya)
    return pts[-1][0]


def outer_wall():
    sk = (cq.Workplane("XY")
          .moveTo(*TAPER_OUT[0])
          .spline(TAPER_OUT[1:], tangents=[(0, 1), (0.17, 1)], includeCurrent=True)
          .spline(FLARE_OUT[1:], tangents=[(0, 1), (-0.3, 1)], includeCurrent=True)
          .lineTo(*FLARE_IN[0])
          .spline(FLARE_IN[1:], tangents=[(0.05, -1), (0, -1)], includeCurrent=True)
          .lineTo(WO - T, TAPER_Y)
          .spline(list(reversed(TAPER_IN))[1:], tangents=[(-0.17, -1), (0, -1)],
                  includeCurrent=True)
          .close())
    return sk.extrude(H)


def half_clip(with_window):
    """Right-hand half of one clip (unit-relative x >= 0)."""
    bx0, bx1 = BLADE_X
    wall = outer_wall()

    # ---- low inner bar from the blade to the lower rib ----
    def x_bar_in(y):
        return BAR_TIP_X + (BAR_IN_X - BAR_TIP_X) * (y - BAR_Y0) / (RIB1_Y[1] - BAR_Y0)

    bar = poly_prism([(bx0, BAR_Y0 - 3.0), (bx1 - 0.3, BAR_Y0 - 3.0),
                      (BAR_IN_X + BAR_W, RIB1_Y[1]), (BAR_IN_X, RIB1_Y[1]),
                      (BAR_TIP_X, BAR_Y0)], 0, BAR_H)

    # ---- gusset filling the V behind the blade: steep top, high at the wall ----
    yb = GUSSET_Y
    xw_b = interp(TAPER_IN, yb)
    g_pts = [(bx0, BAR_Y0 - 3.0), (bx1 - 0.3, BAR_Y0 - 3.0),
             (xw_b + 0.4, yb), (x_bar_in(yb), yb), (BAR_TIP_X, BAR_Y0)]
    gus = poly_prism(g_pts, 0, H)
    r1 = cq.Vector(x_bar_in(yb), yb, BAR_H)
    r2 = cq.Vector(xw_b, yb, BAR_H + GUS_RISE)
    r3 = cq.Vector(BAR_TIP_X, BAR_Y0, ZC)
    nrm = (r2 - r1).cross(r3 - r1).normalized()
    if nrm.z < 0:
        nrm = -nrm
    cut_pl = cq.Plane(origin=r1, xDir=(r2 - r1).normalized(), normal=nrm)
    gcut = cq.Workplane(cut_pl).rect(80, 80).extrude(40)
    gus = gus.cut(gcut)

    # ---- low ribs with small holes ----
    def rib(y0, y1):
        r = poly_prism([(BAR_IN_X + RIB_CH, y0), (WO - T + 0.5, y0),
                        (WO - T + 0.5, y1), (BAR_IN_X + RIB_CH, y1),
                        (BAR_IN_X, y1 - RIB_CH), (BAR_IN_X, y0 + RIB_CH)], 0, BAR_H)
        hole = (cq.Workplane("XY").center(PEG_X, (y0 + y1) / 2)
                .circle(RIB_HOLE_D / 2).extrude(BAR_H))
        return r.cut(hole)

    rib1 = rib(*RIB1_Y)
    rib2 = rib(*RIB2_Y)

    # ---- box under the plate (hollow, open at the bottom; notch on one half) ----
    py0, py1 = PLATE_Y
    box = poly_prism([(BOX_X0, py0), (WO - T + 0.5, py0),
                      (WO - T + 0.5, py1), (BOX_X0, py1)], 0, H)
    cavity = poly_prism([(BOX_X0 + BOX_WALL, py0 + BOX_WALL), (WO - T, py0 + BOX_WALL),
                         (WO - T, py1 - BOX_WALL), (BOX_X0 + BOX_WALL, py1 - BOX_WALL)],
                        -1, H - BOX_WALL)
    box = box.cut(cavity)
    if with_window:
        window = poly_prism([(BOX_X0 - 1, py0 - 1), (BOX_X0 + WIN[0], py0 - 1),
                             (BOX_X0 + WIN[0], py0 + WIN[1]), (BOX_X0 - 1, py0 + WIN[1])],
                            WIN[2], H)
        box = box.cut(window)

    # ---- sloped gusset along the wall between plate box and flared end ----
    gus_profile = [(WO - T, H), (GUS_X, BAR_H), (WO - T + 0.5, BAR_H), (WO - T + 0.5, H)]
    gus2 = xz_prism(gus_profile, py1 - 0.5, GUS2_Y1)

    # ---- sloped gusset in front of the box, cut off by a diagonal face ----
    gus_f = xz_prism([(WO - T, H), (GUSF_X, BAR_H), (WO - T + 0.5, BAR_H), (WO - T + 0.5, H)],
                     GUSF_Y0 - 4.0, py0 + 0.5)
    k = (py0 - GUSF_WALL_Y) / (GUSF_X - (WO - T))        # dY/dx of the diagonal
    xa, xb = WO + 1.0, BOX_X0 - 1.0
    ya = GUSF_WALL_Y + k * (xa - (WO - T))
    yb = GUSF_WALL_Y + k * (xb - (WO - T))
    diag_cut = poly_prism([(xa, ya), (xb, yb), (xb, GUSF_Y0 - 10), (xa, GUSF_Y0 - 10)],
                          -1, H + 1)
    gus_f = gus_f.cut(diag_cut)

    # ---- peg plate ----
    plate = poly_prism([(PLATE_END_X, py0), (WO - T + 0.3, py0),
                        (WO - T + 0.3, py1), (PLATE_END_X, py1)], H, H + PLATE_T)
    plate = plate.edges("|Z and <X").fillet(PLATE_R)
    bev_cut = xz_prism([(PLATE_FLAT_X, H + PLATE_T), (WO - T + 0.3, H),
                        (WO + 1, H), (WO + 1, H + PLATE_T + 1),
                        (PLATE_FLAT_X, H + PLATE_T + 1)], py0 - 1, py1 + 1)
    plate = plate.cut(bev_cut)
    plate = (plate.edges("|Y")
             .edges(cq.selectors.BoxSelector((PLATE_FLAT_X - 0.2, py0 - 1, H + PLATE_T - 0.2),
                                             (PLATE_FLAT_X + 0.2, py1 + 1, H + PLATE_T + 0.2)))
             .fillet(BEV_R))
    peg = (cq.Workplane("XY").workplane(offset=H + PLATE_T)
           .center(PEG_X, PEG_Y).circle(PEG_D / 2).extrude(PEG_H))

    body = (wall.union(bar).union(gus).union(rib1).union(rib2).union(box)
            .union(gus2).union(gus_f).union(plate).union(peg))

    # ---- chevron cuts at both ends (side view) ----
    x0, x1 = -5.0, 30.0
    tip_top = yz_prism([(0.0, ZC), (TIP_CHEV, H), (TIP_CHEV, H + 20),
                        (-5, H + 20), (-5, ZC)], x0, x1)
    tip_bot = yz_prism([(0.0, ZC), (TIP_CHEV, 0.0), (TIP_CHEV, -20),
                        (-5, -20), (-5, ZC)], x0, x1)
    end_top = yz_prism([(L, ZC_END), (L - END_CHEV, H), (L - END_CHEV, H + 20),
                        (L + 5, H + 20), (L + 5, ZC_END)], x0, x1)
    end_bot = yz_prism([(L, ZC_END), (L - END_CHEV, 0.0), (L - END_CHEV, -20),
                        (L + 5, -20), (L + 5, ZC_END)], x0, x1)
    body = body.cut(tip_top).cut(tip_bot).cut(end_top).cut(end_bot)
    return body


right = half_clip(True)
left = half_clip(False).mirror("YZ")
unit = right.union(left)

result = None
for i in range(N_UNITS):
    u = unit.translate(((i - (N_UNITS - 1) / 2) * PITCH, -L / 2, 0))
    result = u if result is None else result.union(u)

VIEW = {"azimuth": 45, "elevation": 26}
